import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_IN = 31.0          # inner radius of the C (hook) opening
R_OUT = 56.6         # outer radius of the C ring
TIP_ANG = 67.5       # angular position of the rounded C tips (deg, +/-)
T_RING = 29.0        # thickness of the C ring (along +Y)
T_PLATE = 6.6        # thickness of the flat handle plate
HANDLE_LEN = 207.5  # ring centre -> extreme tip of the handle
TIP_R = 6.6          # end radius of the handle tip
HALF_ANG = 9.0       # half taper angle of the handle (deg)
FILLET_R = 65.0      # blend radius between handle edge and ring

HOLE_STEP = 22.5     # angular pitch of the hole pattern (deg)
N_HOLES = 11
D_SMALL = 6.7
D_LARGE = 9.3
R_SMALL = 43.8       # pitch radius of the small holes
R_LARGE = 46.0       # pitch radius of the large holes

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
R_MID = 0.5 * (R_IN + R_OUT)
R_CAP = 0.5 * (R_OUT - R_IN)


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def add(p, q, s=1.0):
    return (p[0] + s * q[0], p[1] + s * q[1])


a = math.radians(HALF_ANG)
n_up = (-math.sin(a), math.cos(a))          # outward normal of upper handle edge
tip_c = (-HANDLE_LEN + TIP_R, 0.0)
d_line = n_up[0] * tip_c[0] + n_up[1] * tip_c[1] + TIP_R

# blend point on outer circle: sin(theta - a) = (d + rf) / (R + rf)
s = (d_line + FILLET_R) / (R_OUT + FILLET_R)
theta_b = math.degrees(a) + 180.0 - math.degrees(math.asin(s))
fc = pol(R_OUT + FILLET_R, theta_b)                 # fillet centre (upper)
B_top = pol(R_OUT, theta_b)                         # fillet / ring tangency
T_top = add(fc, n_up, -FILLET_R)                    # fillet / line tangency
U_top = add(tip_c, n_up, TIP_R)                     # line / tip tangency


def mir(p):
    return (p[0], -p[1])


def fillet_mid(p0, p1, c, r):
    m = ((p0[0] + p1[0]) / 2 - c[0], (p0[1] + p1[1]) / 2 - c[1])
    L = math.hypot(*m)
    return (c[0] + r * m[0] / L, c[1] + r * m[1] / L)


f_mid = fillet_mid(B_top, T_top, fc, FILLET_R)
tip_left = (-HANDLE_LEN, 0.0)

# cap (rounded tip of the C) points
cap_top_c = pol(R_MID, TIP_ANG)
cap_top_mid = add(cap_top_c, pol(R_CAP, TIP_ANG - 90.0))
cap_bot_c = pol(R_MID, -TIP_ANG)
cap_bot_mid = add(cap_bot_c, pol(R_CAP, -TIP_ANG + 90.0))


def ring_band(wp):
    """C-shaped band: outer arc, rounded cap, inner arc, rounded cap."""
    return (
        wp.moveTo(*pol(R_OUT, TIP_ANG))
        .threePointArc(pol(R_OUT, 180.0), pol(R_OUT, -TIP_ANG))
        .threePointArc(cap_bot_mid, pol(R_IN, -TIP_ANG))
        .threePointArc(pol(R_IN, 180.0), pol(R_IN, TIP_ANG))
        .threePointArc(cap_top_mid, pol(R_OUT, TIP_ANG))
        .close()
    )


# full flat outline (ring + handle with blends)
plate = (
    cq.Workplane("XZ")
    .moveTo(*pol(R_OUT, TIP_ANG))
    .threePointArc(pol(R_OUT, 0.5 * (TIP_ANG + theta_b)), B_top)
    .threePointArc(f_mid, T_top)
    .lineTo(*U_top)
    .threePointArc(tip_left, mir(U_top))
    .lineTo(*mir(T_top))
    .threePointArc(mir(f_mid), mir(B_top))
    .threePointArc(pol(R_OUT, -0.5 * (TIP_ANG + theta_b)), pol(R_OUT, -TIP_ANG))
    .threePointArc(cap_bot_mid, pol(R_IN, -TIP_ANG))
    .threePointArc(pol(R_IN, 180.0), pol(R_IN, TIP_ANG))
    .threePointArc(cap_top_mid, pol(R_OUT, TIP_ANG))
    .close()
    .extrude(-T_PLATE)
)

ring = ring_band(cq.Workplane("XZ")).extrude(-T_RING)

body = plate.union(ring)

# hole pattern: alternating small / large holes around the C
pts_small = []
pts_large = []
for i in range(N_HOLES):
    ang = TIP_ANG + i * HOLE_STEP
    if i % 2 == 0:
        pts_small.append(pol(R_SMALL, ang))
    else:
        pts_large.append(pol(R_LARGE, ang))

cut_small = (
    cq.Workplane("XZ").workplane(offset=1.0)
    .pushPoints(pts_small).circle(D_SMALL / 2).extrude(-(T_RING + 2.0))
)
cut_large = (
    cq.Workplane("XZ").workplane(offset=1.0)
    .pushPoints(pts_large).circle(D_LARGE / 2).extrude(-(T_RING + 2.0))
)

result = body.cut(cut_small).cut(cut_large)
